import cadquery as cq

# =====================================================================
#  Mounting plate: thin rounded-rectangle plate standing in the XZ plane
#  (thickness along +Y).  Flat front face (-Y) with six through holes;
#  the back face (+Y) carries a filleted boss around every hole plus
#  four shallow blind locating holes near the top / bottom edges.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 300.0            # plate width  (X)
H = 185.0            # plate height (Z)
T = 4.5              # plate thickness (Y)
R_CORNER = 24.5      # corner radius of the outline
EDGE_CHAMFER = 0.5   # small chamfer on the back-face perimeter edge

HOLE_D = 4.5         # through-hole diameter
HOLE_CHAMFER = 0.75  # chamfer at the hole mouth on the boss top
BOSS_D = 11.0        # boss diameter (back face)
BOSS_H = 4.0         # boss height above the back face
BOSS_BASE_FILLET = 1.8

BLIND_D = 6.0        # shallow blind holes on the back face
BLIND_DEPTH = 1.0

# through holes with bosses, (X, Z) as seen in the front view
HOLES = [
    (-130.3, 42.9),
    (130.7, 58.3),
    (0.0, 19.2),
    (4.5, -50.9),
    (-130.3, -72.7),
    (92.4, -72.7),
]

# blind holes (back face only), symmetric pattern near top/bottom edges
BLIND_X = 94.6
BLIND_Z = 86.1
BLIND = [(sx * BLIND_X, sz * BLIND_Z) for sx in (1, -1) for sz in (1, -1)]

VIEW = {"azimuth": 45, "elevation": 26}


def back_plane(y):
    """Workplane parallel to the plate at depth y.  The XZ plane normal
    is -Y, so a negative extrude grows toward +Y (toward the back)."""
    return cq.Workplane("XZ", origin=(0, y, 0))


# ---------------- plate ----------------
plate = (
    back_plane(0)
    .rect(W, H)
    .extrude(-T)
    .edges("|Y")
    .fillet(R_CORNER)
)
# edge break on the back-face perimeter
plate = plate.faces(">Y").edges().chamfer(EDGE_CHAMFER)

# ---------------- bosses on the back (+Y) face ----------------
bosses = (
    back_plane(T)
    .pushPoints(HOLES)
    .circle(BOSS_D / 2.0)
    .extrude(-BOSS_H)
)
plate = plate.union(bosses)


def _is_boss_base(e):
    """Circular edge of boss radius lying in the back-face plane."""
    return (
        e.geomType() == "CIRCLE"
        and abs(e.radius() - BOSS_D / 2.0) < 1e-3
        and abs(e.Center().y - T) < 1e-3
    )


plate = (
    plate.edges(cq.selectors.BoxSelector((-W, T - 0.01, -H), (W, T + 0.01, H)))
    .filter(_is_boss_base)
    .fillet(BOSS_BASE_FILLET)
)

# ---------------- through holes ----------------
cutter = (
    back_plane(-1.0)
    .pushPoints(HOLES)
    .circle(HOLE_D / 2.0)
    .extrude(-(T + BOSS_H + 2.0))
)
plate = plate.cut(cutter)

# chamfer the hole mouths on the boss tops (smallest circles on the top faces)
plate = (
    plate.faces(">Y")
    .edges("%CIRCLE")
    .edges(cq.selectors.RadiusNthSelector(0))
    .chamfer(HOLE_CHAMFER)
)

# ---------------- shallow blind holes on the back face ----------------
blind = (
    back_plane(T - BLIND_DEPTH)
    .pushPoints(BLIND)
    .circle(BLIND_D / 2.0)
    .extrude(-(BLIND_DEPTH + 1.0))
)
plate = plate.cut(blind)

result = plate
